import math
import cadquery as cq
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.gp import gp_Pnt
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge

# ---------------- driving dimensions (mm) ----------------
L = 108.0            # overall length (Y)
H = 24.5             # overall height (Z)
R_CORNER = 5.0       # nominal corner radius of the housing outline (YZ)
SOFT_A = 8.8         # reach of the curvature-continuous corner blend
D_FRONT = 8.0        # depth of the front frame (X)
D_BACK = 4.4         # depth of the rounded back cover (X)
BACK_INSET = 0.56    # back cover inset from the frame outline
R_BACK = 4.0         # big round on the back cover

PANEL_INSET = 1.0    # inner front panel outline inset
PANEL_DEPTH = 0.08   # very shallow step

LENS_Y = (-23.0, 41.0)   # lens centres along Y (64 mm baseline)
BAND_R = 8.9             # half-height of the recessed band joining the lenses
BAND_DEPTH = 0.8
DISC_R = 8.4             # lens disc radius
DISC_TOP = 0.35          # disc top below the front face
DISC_CH = 0.3            # chamfer on the disc top edge
COLLAR_R = 4.6           # lens collar (12-sided, circumradius)
COLLAR_TOP = 0.0        # collar top below the front face
COLLAR_CH = 0.08         # tiny break on the collar top edge
RING_R = 3.3             # inner edge of the collar
NOTCH_R = 3.85           # four notches reaching out to this radius
NOTCH_W = 1.8
RING_DEPTH = 0.5         # step below the collar top
BORE_R = 2.55            # lens bore
BORE_DEPTH = 1.1         # below the front face
LENS_R = 2.45            # fisheye lens radius
LENS_TOP = 0.12          # lens top below the front face
LENS_FILLET = 0.45       # rounded flank of the lens

WEDGE_DEPTH = 0.08       # shallow wedge in the left lens disc
WEDGE_HALF_ANGLE = 25.0

# tapered strip below the logo on the front face (very shallow)
STRIP_TOP_Z = -1.6
STRIP_BOT_Z = -11.0
STRIP_TOP_Y = (-51.5, -47.6)
STRIP_BOT_Y = (-50.9, -49.1)
STRIP_DEPTH = 0.05

SLOT_LEN = 12.9          # connector slot on the -Y end
SLOT_W = 3.0
SLOT_DEPTH = 5.0
END_HOLE_D = 1.6
END_HOLE_Z = 9.05
END_HOLE_DEPTH = 3.0

BACK_HOLE_D = 2.0
BACK_HOLE_Y = (-25.0, 25.0)

XF = D_FRONT  # x of the front face

# ---------------- helpers ----------------
def soft_outline(x0, hy, hz, a):
    """Closed, curvature-continuous rounded-rectangle outline in the plane X = x0.

    Periodic cubic B-spline whose control polygon is the rectangle |Y|<=hy,
    |Z|<=hz with extra control points at a and 2a from the corners, so the long
    sides are exactly straight and the corners blend smoothly (no tangent seams).
    """
    pts = [
        (hy, -hz + a), (hy, hz - a), (hy, hz),
        (hy - a, hz), (hy - 2 * a, hz), (-hy + 2 * a, hz), (-hy + a, hz), (-hy, hz),
        (-hy, hz - a), (-hy, -hz + a), (-hy, -hz),
        (-hy + a, -hz), (-hy + 2 * a, -hz), (hy - 2 * a, -hz), (hy - a, -hz), (hy, -hz),
    ]
    n = len(pts)
    poles = TColgp_Array1OfPnt(1, n)
    for k, (y, z) in enumerate(pts):
        poles.SetValue(k + 1, gp_Pnt(x0, y, z))
    knots = TColStd_Array1OfReal(1, n + 1)
    mults = TColStd_Array1OfInteger(1, n + 1)
    for k in range(n + 1):
        knots.SetValue(k + 1, float(k))
        mults.SetValue(k + 1, 1)
    crv = Geom_BSplineCurve(poles, knots, mults, 3, True)
    edge = cq.Edge(BRepBuilderAPI_MakeEdge(crv).Edge())
    return cq.Wire.assembleEdges([edge])


def soft_slab(x0, depth, hy, hz, a):
    wire = soft_outline(x0, hy, hz, a)
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(wire, [], cq.Vector(depth, 0, 0)))


# ---------------- housing ----------------
frame = soft_slab(0.0, D_FRONT, L / 2, H / 2, SOFT_A)

back = (
    cq.Workplane("YZ", origin=(-D_BACK, 0, 0))
    .rect(L - 2 * BACK_INSET, H - 2 * BACK_INSET)
    .extrude(D_BACK)
    .edges("|X")
    .fillet(R_CORNER - BACK_INSET)
)
back = back.faces("<X").edges().fillet(R_BACK)

body = frame.union(back)

# ---------------- front face details ----------------
# inner panel outline (very shallow step)
panel = soft_slab(
    XF - PANEL_DEPTH, 1.0, L / 2 - PANEL_INSET, H / 2 - PANEL_INSET, SOFT_A - PANEL_INSET
)
body = body.cut(panel)

# recessed band joining the two lenses
yc = 0.5 * (LENS_Y[0] + LENS_Y[1])
span = LENS_Y[1] - LENS_Y[0]
band = (
    cq.Workplane("YZ", origin=(XF - BAND_DEPTH, 0, 0))
    .center(yc, 0)
    .slot2D(span + 2 * BAND_R, 2 * BAND_R, 0)
    .extrude(1.0)
)
body = body.cut(band)

for i, ly in enumerate(LENS_Y):
    # lens disc rising from the band floor, softened top edge
    disc = (
        cq.Workplane("YZ", origin=(XF - BAND_DEPTH, ly, 0))
        .circle(DISC_R)
        .extrude(BAND_DEPTH - DISC_TOP)
        .faces(">X")
        .edges()
        .chamfer(DISC_CH)
    )
    body = body.union(disc)

    if i == 0:
        # shallow wedge between the collar and the disc edge (towards -Y)
        th = math.radians(WEDGE_HALF_ANGLE)
        rr = DISC_R + 1.0
        wedge = (
            cq.Workplane("YZ", origin=(XF - DISC_TOP - WEDGE_DEPTH, 0, 0))
            .polyline(
                [
                    (ly, 0),
                    (ly - rr * math.cos(th), rr * math.sin(th)),
                    (ly - rr * math.cos(th), -rr * math.sin(th)),
                ]
            )
            .close()
            .extrude(1.0)
        )
        wedge = wedge.intersect(
            cq.Workplane("YZ", origin=(XF - 2.0, ly, 0))
            .circle(DISC_R - DISC_CH)
            .extrude(3.0)
        )
        body = body.cut(wedge)

    # faceted collar
    collar_base = XF - DISC_TOP - 0.1
    collar = (
        cq.Workplane("YZ", origin=(collar_base, ly, 0))
        .polygon(12, 2 * COLLAR_R)
        .extrude(XF - COLLAR_TOP - collar_base)
        .faces(">X")
        .edges()
        .chamfer(COLLAR_CH)
    )
    body = body.union(collar)

    # notched ring inside the collar
    ring_floor = XF - COLLAR_TOP - RING_DEPTH
    ring = (
        cq.Workplane("YZ", origin=(ring_floor, ly, 0))
        .circle(RING_R)
        .extrude(2.0)
    )
    for k in range(4):
        a = k * 90.0
        notch = (
            cq.Workplane("YZ", origin=(ring_floor, ly, 0))
            .transformed(rotate=(0, 0, a))
            .center(0.5 * (RING_R + NOTCH_R) - 0.3, 0)
            .rect(NOTCH_R - RING_R + 0.6, NOTCH_W)
            .extrude(2.0)
        )
        ring = ring.union(notch)
    body = body.cut(ring)

    # lens bore
    bore = (
        cq.Workplane("YZ", origin=(XF - BORE_DEPTH, ly, 0))
        .circle(BORE_R)
        .extrude(2.0)
    )
    body = body.cut(bore)

    # fisheye lens: flat-topped with a strongly rounded flank
    lens_base = XF - BORE_DEPTH - 0.05
    dome = (
        cq.Workplane("YZ", origin=(lens_base, ly, 0))
        .circle(LENS_R)
        .extrude(XF - LENS_TOP - lens_base)
        .faces(">X")
        .edges()
        .fillet(LENS_FILLET)
    )
    body = body.union(dome)

# tapered strip below the logo
strip = (
    cq.Workplane("YZ", origin=(XF - PANEL_DEPTH - STRIP_DEPTH, 0, 0))
    .polyline(
        [
            (STRIP_TOP_Y[0], STRIP_TOP_Z),
            (STRIP_TOP_Y[1], STRIP_TOP_Z),
            (STRIP_BOT_Y[1], STRIP_BOT_Z),
            (STRIP_BOT_Y[0], STRIP_BOT_Z),
        ]
    )
    .close()
    .extrude(1.0)
)
body = body.cut(strip)

# ---------------- -Y end: connector slot and two holes ----------------
end_wp = cq.Workplane("XZ", origin=(0, -L / 2 - 1.0, 0))  # start the tools outside the end
slot = (
    end_wp.center(D_FRONT / 2, 0)
    .slot2D(SLOT_LEN, SLOT_W, 90)
    .extrude(-(SLOT_DEPTH + 1.0))
)
body = body.cut(slot)
holes = (
    end_wp.pushPoints([(D_FRONT / 2, END_HOLE_Z), (D_FRONT / 2, -END_HOLE_Z)])
    .circle(END_HOLE_D / 2)
    .extrude(-(END_HOLE_DEPTH + 1.0))
)
body = body.cut(holes)

# ---------------- back: two mounting holes ----------------
bh = (
    cq.Workplane("YZ", origin=(-D_BACK - 0.1, 0, 0))
    .pushPoints([(y, 0) for y in BACK_HOLE_Y])
    .circle(BACK_HOLE_D / 2)
    .extrude(3.0)
)
body = body.cut(bh)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
